import math
import cadquery as cq
from cadquery.occ_impl.shapes import BRepFilletAPI_MakeFillet, TopExp  # OCC kernel classes used by cadquery

# ---------------------------------------------------------------- parameters (mm)
# U-shaped fork (two arms + web); X runs from the arm tips (-X) to the knob (+X),
# the web outer face is at X=0, the part is symmetric about Y=0 and (before tilt) Z=0.
WEB_T = 3.05            # web thickness
WEB_HALF_W = 12.45      # half width of the web (Y)
ARM_TIP_X = -53.5       # arm tip
PAD_CX = -42.8          # centre of the round arm pad (hole centre)
PAD_R = 10.8            # radius of the round pad at the arm tip
PAD_TAN_DEG = 78.0      # where the arm side edge leaves the pad circle
# arm side edge in the top view (x, half width), from the web towards the pad
PLAN_PTS = [(-4.5, 12.43), (-8.1, 11.65), (-14.2, 10.25), (-20.35, 9.5), (-26.45, 9.33), (-32.55, 9.5)]
# outer / inner faces of the arms: gentle arcs through three (x, z) points each
ARM_OUT_PTS = [(-53.5, 19.4), (-31.75, 20.15), (-9.45, 21.7)]
ARM_IN_PTS = [(-53.5, 16.2), (-31.75, 16.65), (-9.45, 17.95)]
R_BEND_OUT = 8.35
R_BEND_IN = 5.8
EDGE_FILLET_OUT = 1.4   # rounding of the outer side edges of the U
EDGE_FILLET_IN = 1.4    # rounding of the inner side edges of the U ...
EDGE_FILLET_IN_PAD = 0.4  # ... fading to this radius at the pad centre
EDGE_FADE_X = -9.3      # x where the inner rounding reaches its full radius

# holes in the arm pads
ARM_HOLE_D = 5.75
ARM_BOLT_R = 6.75
ARM_BOLT_D = 1.1
ARM_CBORE_D = 2.5
ARM_CBORE_DEPTH = 1.3

# holes in the web (on the Y and Z axes around the shaft)
WEB_HOLE_R = 7.05
WEB_HOLE_D = 1.3
WEB_CSK_D = 3.8         # countersink of the Z-axis web holes at the end of the slot

# shaft: smooth loft from a rounded square at the web to the round neck
SHAFT_SECTIONS = [      # (x, half width, corner radius); r >= half -> round section
    (0.0, 9.3, 2.1),
    (4.5, 9.15, 2.6),
    (20.0, 6.65, 4.6),
    (32.0, 4.65, 4.65),
    (48.7, 3.85, 3.85),
]

# knob at the end of the shaft
KNOB_X0 = 48.7
CONE_R0 = 5.33
CONE_R1 = 7.45
CONE_END_X = 60.6
GROOVE_W = 0.6
GROOVE_D = 0.35
RIM_R = 7.6
RIM_END_X = 63.45
RIM_FILLET = 2.2
BOSS_R = 4.95
BOSS_END_X = 64.75
BOSS_CHAMFER = 0.2
STEP_R = 4.0            # small raised disc on the boss face
STEP_H = 0.25
RECESS_R = 2.05
RECESS_D = 0.6

# through slot (along Z) in the shaft near the web
SLOT_X0 = 1.95
SLOT_X1 = 19.3
SLOT_W = 4.3

# four lens-shaped flank grooves, cut by a 'lemon' (circular arc revolved about its chord)
# lying along each flank, its axis parallel to the flank and slightly outside it
GROOVE_X0 = 3.25        # groove ends on the flank (used to align the lemon with the flank)
GROOVE_X1 = 29.6
LEMON_XC = 17.5         # centre of the lemon
LEMON_LEN = 36.5        # chord length of the lemon
LEMON_R = 2.25          # max radius of the lemon
LEMON_OFF = 1.0         # lemon axis distance outside the flank

TILT_DEG = 0.8          # the whole part is tilted slightly about Y (knob end down)

# measured half width of the shaft flanks (x, half width) used to place the grooves
FLANK = [(0.5, 9.25), (4.3, 9.2), (9.1, 8.5), (13.9, 7.8), (18.0, 7.0), (22.9, 6.2),
         (27.7, 5.35), (30.5, 4.8), (32.5, 4.5), (34.4, 4.3), (37.3, 3.95), (42.1, 3.75)]


def flank(x):
    for (x0, h0), (x1, h1) in zip(FLANK[:-1], FLANK[1:]):
        if x0 <= x <= x1:
            return h0 + (h1 - h0) * (x - x0) / (x1 - x0)
    return FLANK[0][1] if x < FLANK[0][0] else FLANK[-1][1]


# ---------------------------------------------------------------- U-shaped fork
def circle3(p1, p2, p3):
    """centre and radius of the circle through three 2D points"""
    (x1, y1), (x2, y2), (x3, y3) = p1, p2, p3
    d = 2 * (x1 * (y2 - y3) + x2 * (y3 - y1) + x3 * (y1 - y2))
    ux = ((x1 ** 2 + y1 ** 2) * (y2 - y3) + (x2 ** 2 + y2 ** 2) * (y3 - y1) + (x3 ** 2 + y3 ** 2) * (y1 - y2)) / d
    uy = ((x1 ** 2 + y1 ** 2) * (x3 - x2) + (x2 ** 2 + y2 ** 2) * (x1 - x3) + (x3 ** 2 + y3 ** 2) * (x2 - x1)) / d
    return (ux, uy), math.hypot(x1 - ux, y1 - uy)


def arc_z(pts, x):
    """height of the (concave-up) arc through pts at abscissa x"""
    (cx, cz), r = circle3(*pts)
    return cz - math.sqrt(r * r - (x - cx) ** 2)


X_TAIL = ARM_TIP_X - 1.0            # profile runs past the tip, the plan-form trims it
z_corner_o = arc_z(ARM_OUT_PTS, 0.0)
z_corner_i = arc_z(ARM_IN_PTS, -WEB_T)
z_tip_o = arc_z(ARM_OUT_PTS, X_TAIL)
z_tip_i = arc_z(ARM_IN_PTS, X_TAIL)
xm_o, xm_i = ARM_OUT_PTS[1][0], ARM_IN_PTS[1][0]
zm_o, zm_i = arc_z(ARM_OUT_PTS, xm_o), arc_z(ARM_IN_PTS, xm_i)
ARM_PAD_Z = arc_z(ARM_OUT_PTS, PAD_CX)   # outer face height at the pad centre

u_body = (
    cq.Workplane("XZ")
    .moveTo(X_TAIL, z_tip_o)
    .threePointArc((xm_o, zm_o), (0.0, z_corner_o))
    .lineTo(0.0, -z_corner_o)
    .threePointArc((xm_o, -zm_o), (X_TAIL, -z_tip_o))
    .lineTo(X_TAIL, -z_tip_i)
    .threePointArc((xm_i, -zm_i), (-WEB_T, -z_corner_i))
    .lineTo(-WEB_T, z_corner_i)
    .threePointArc((xm_i, zm_i), (X_TAIL, z_tip_i))
    .close()
    .extrude(WEB_HALF_W + 2.0, both=True)
)
u_body = u_body.edges(cq.selectors.NearestToPointSelector((0.0, 0.0, z_corner_o))).fillet(R_BEND_OUT)
u_body = u_body.edges(cq.selectors.NearestToPointSelector((0.0, 0.0, -z_corner_o))).fillet(R_BEND_OUT)
u_body = u_body.edges(cq.selectors.NearestToPointSelector((-WEB_T, 0.0, z_corner_i))).fillet(R_BEND_IN)
u_body = u_body.edges(cq.selectors.NearestToPointSelector((-WEB_T, 0.0, -z_corner_i))).fillet(R_BEND_IN)

# plan-form of the arms (top view): round pad, waist, flare into the web
ang = math.radians(PAD_TAN_DEG)
tp = (PAD_CX + PAD_R * math.cos(ang), PAD_R * math.sin(ang))
tan_in = (-math.sin(ang), math.cos(ang))
side_pts = PLAN_PTS + [tp]
plan = (
    cq.Workplane("XY")
    .moveTo(3.0, -WEB_HALF_W)
    .lineTo(3.0, WEB_HALF_W)
    .lineTo(-0.5, WEB_HALF_W)
    .spline(side_pts, tangents=[(-1.0, 0.0), tan_in], includeCurrent=True)
    .threePointArc((PAD_CX - PAD_R, 0.0), (tp[0], -tp[1]))
    .spline([(p[0], -p[1]) for p in reversed(side_pts[:-1])] + [(-0.5, -WEB_HALF_W)],
            tangents=[(-tan_in[0], tan_in[1]), (1.0, 0.0)], includeCurrent=True)
    .close()
    .extrude(30.0, both=True)
)

fork = u_body.intersect(plan).val()

# rounded side edges of the U: constant radius on the outer surface all around, and on the
# inner surface a radius that fades out towards the pads (nearly sharp inner pad edges)


def _is_y_line(e):
    return e.geomType() == "LINE" and abs(e.tangentAt(0.5).y) > 0.99


def _inner_edge(e):
    c = e.Center()
    return not _is_y_line(e) and (
        abs(c.x + WEB_T) < 0.5 or (c.x < -WEB_T - 0.5 and 15.0 < abs(c.z) < 18.9))


def _outer_edge(e):
    c = e.Center()
    return not _is_y_line(e) and (c.x > -1.5 or abs(c.z) > 18.9)


def _inner_r(x):
    t = (x - PAD_CX) / (EDGE_FADE_X - PAD_CX)
    return EDGE_FILLET_IN_PAD + (EDGE_FILLET_IN - EDGE_FILLET_IN_PAD) * max(0.0, min(1.0, t))


def _fillet(shape, select, radius, radius_law=None):
    """fillet the selected edges (tangent chains propagate); optional per-edge radius law
    r(x) evaluated at the edge end points. Falls back to a constant radius, then to no fillet."""
    for law in ((radius_law, None) if radius_law else (None,)):
        mk = BRepFilletAPI_MakeFillet(shape.wrapped)
        for e in shape.Edges():
            if select(e):
                mk.Add(radius, e.wrapped)
        if law is not None:
            for ic in range(1, mk.NbContours() + 1):
                for ie in range(1, mk.NbEdges(ic) + 1):
                    ed = mk.Edge(ic, ie)
                    x_first = cq.Vertex(TopExp.FirstVertex_s(ed)).toTuple()[0]
                    x_last = cq.Vertex(TopExp.LastVertex_s(ed)).toTuple()[0]
                    mk.SetRadius(law(x_last), law(x_first), ic, ie)
        try:
            mk.Build()
            if mk.IsDone():
                out = cq.Shape.cast(mk.Shape())
                if out.isValid():
                    return out
        except Exception:
            pass
    return shape


fork = _fillet(fork, _inner_edge, EDGE_FILLET_IN, _inner_r)
fork = _fillet(fork, _outer_edge, EDGE_FILLET_OUT)
fork = cq.Workplane("XY").add(fork)

# holes in the arm pads: central hole + 4 counterbored holes from the outside
bolt_pts = [(PAD_CX + ARM_BOLT_R, 0.0), (PAD_CX - ARM_BOLT_R, 0.0),
            (PAD_CX, ARM_BOLT_R), (PAD_CX, -ARM_BOLT_R)]
holes = (
    cq.Workplane("XY").workplane(offset=-30.0)
    .center(PAD_CX, 0.0).circle(ARM_HOLE_D / 2).extrude(60.0)
)
for (x, y) in bolt_pts:
    holes = holes.union(
        cq.Workplane("XY").workplane(offset=-30.0).center(x, y).circle(ARM_BOLT_D / 2).extrude(60.0)
    )
    for z0 in (ARM_PAD_Z - ARM_CBORE_DEPTH, -ARM_PAD_Z - 1.0):
        cb = (
            cq.Workplane("XY").workplane(offset=z0)
            .center(x, y).circle(ARM_CBORE_D / 2).extrude(ARM_CBORE_DEPTH + 1.0)
        )
        holes = holes.union(cb)
fork = fork.cut(holes)

# ---------------------------------------------------------------- shaft


def section_wire(x, h, r, beta_deg=20.0):
    """8-edge closed section at X=x in the YZ plane: rounded square (half width h, corner
    radius r), or a circle of radius h split into 8 arcs the same way when r >= h."""
    V = lambda y, z: cq.Vector(x, y, z)
    edges = []
    if r < h - 1e-6:
        a = h - r
        c = r * (1 - 1 / math.sqrt(2))
        pts = [(h, -a), (h, a), (a, h), (-a, h), (-h, a), (-h, -a), (-a, -h), (a, -h)]
        mids = [(h - c, h - c), (-(h - c), h - c), (-(h - c), -(h - c)), (h - c, -(h - c))]
        for i in range(4):
            p0, p1, p2 = pts[2 * i], pts[2 * i + 1], pts[(2 * i + 2) % 8]
            edges.append(cq.Edge.makeLine(V(*p0), V(*p1)))
            edges.append(cq.Edge.makeThreePointArc(V(*p1), V(*mids[i]), V(*p2)))
    else:
        b = math.radians(beta_deg)
        angs = []
        for k in range(4):
            angs += [k * math.pi / 2 - b, k * math.pi / 2 + b]
        for i in range(8):
            a0, a1 = angs[i], angs[(i + 1) % 8]
            if i == 7:
                a1 += 2 * math.pi
            am = 0.5 * (a0 + a1)
            edges.append(cq.Edge.makeThreePointArc(
                V(h * math.cos(a0), h * math.sin(a0)),
                V(h * math.cos(am), h * math.sin(am)),
                V(h * math.cos(a1), h * math.sin(a1))))
    return cq.Wire.assembleEdges(edges)


wires = [section_wire(x, h, r) for (x, h, r) in SHAFT_SECTIONS]
shaft = cq.Workplane("XY").add(cq.Solid.makeLoft(wires, False))

# knob: revolved profile (x, r) with groove ring, rounded rim, end boss and recess
knob_prof = [
    (KNOB_X0 - 0.3, 0.0),
    (KNOB_X0 - 0.3, SHAFT_SECTIONS[-1][1]),
    (KNOB_X0, SHAFT_SECTIONS[-1][1]),
    (KNOB_X0, CONE_R0),
    (CONE_END_X, CONE_R1),
    (CONE_END_X, CONE_R1 - GROOVE_D),
    (CONE_END_X + GROOVE_W, CONE_R1 - GROOVE_D),
    (CONE_END_X + GROOVE_W, RIM_R),
    (RIM_END_X, RIM_R),
    (RIM_END_X, 0.0),
]
knob = (
    cq.Workplane("XY")
    .polyline(knob_prof)
    .close()
    .revolve(360.0, (0, 0, 0), (1, 0, 0))
)
knob = knob.faces(">X").edges().fillet(RIM_FILLET)
boss = (
    cq.Workplane("YZ").workplane(offset=RIM_END_X - 0.2)
    .circle(BOSS_R).extrude(BOSS_END_X - RIM_END_X + 0.2)
    .faces(">X").edges().chamfer(BOSS_CHAMFER)
    .faces(">X").workplane().circle(STEP_R).extrude(STEP_H)
)
knob = knob.union(boss)
recess = (
    cq.Workplane("YZ").workplane(offset=BOSS_END_X + STEP_H - RECESS_D)
    .circle(RECESS_R).extrude(RECESS_D + 1.0)
)
knob = knob.cut(recess)
shaft = shaft.union(knob)

# through slot (top to bottom) near the web
slot = (
    cq.Workplane("XY").workplane(offset=-20.0)
    .center(0.5 * (SLOT_X0 + SLOT_X1), 0.0)
    .slot2D(SLOT_X1 - SLOT_X0, SLOT_W, 0.0)
    .extrude(40.0)
)
shaft = shaft.cut(slot)


# lens grooves: the lemon is built along +X, tilted to follow the flank taper and pushed
# into the -Y flank, then patterned to the four flanks
w0, w1 = flank(GROOVE_X0), flank(GROOVE_X1)
taper = math.atan2(w0 - w1, GROOVE_X1 - GROOVE_X0)
nx, ny = math.sin(taper), -math.cos(taper)          # outward normal of the -Y flank (XY)
lemon = (
    cq.Workplane("XY")
    .moveTo(-LEMON_LEN / 2, 0.0)
    .threePointArc((0.0, LEMON_R), (LEMON_LEN / 2, 0.0))
    .close()
    .revolve(360.0, (-LEMON_LEN / 2, 0, 0), (LEMON_LEN / 2, 0, 0))
    .val()
)
lemon = lemon.rotate(cq.Vector(0, 0, 0), cq.Vector(0, 0, 1), math.degrees(taper))
lemon = lemon.translate(cq.Vector(LEMON_XC + nx * LEMON_OFF, -flank(LEMON_XC) + ny * LEMON_OFF, 0.0))
for k in range(4):
    t = lemon.rotate(cq.Vector(0, 0, 0), cq.Vector(1, 0, 0), 90.0 * k)
    shaft = shaft.cut(cq.Workplane("XY").add(t))

# web holes (through the web into the shaft base / slot)
web_holes = None
for (y, z) in [(WEB_HOLE_R, 0.0), (-WEB_HOLE_R, 0.0), (0.0, WEB_HOLE_R), (0.0, -WEB_HOLE_R)]:
    h = (cq.Workplane("YZ").workplane(offset=-WEB_T - 1.0)
         .center(y, z).circle(WEB_HOLE_D / 2).extrude(WEB_T + 5.0))
    web_holes = h if web_holes is None else web_holes.union(h)

for z in (WEB_HOLE_R, -WEB_HOLE_R):
    h_csk = 0.5 * (WEB_CSK_D - WEB_HOLE_D)
    csk = cq.Solid.makeCone(WEB_HOLE_D / 2, WEB_CSK_D / 2, h_csk,
                            cq.Vector(SLOT_X0 + 0.25 - h_csk, 0.0, z), cq.Vector(1, 0, 0))
    web_holes = web_holes.union(cq.Workplane("XY").add(csk))

part = fork.union(shaft).cut(web_holes)
part = part.rotate((0, 0, 0), (0, 1, 0), TILT_DEG)

result = part
VIEW = {"azimuth": 45, "elevation": 26}
